import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Interlocking puzzle floor tile (solid slab) with compliant spring clips
# ---------------------------------------------------------------------------
L = 200.0            # plate square size (edge to edge, without tabs)
H = 20.0             # slab thickness
RC = 9.0             # plate corner radius
TOP_R = 0.0          # rounding of the slab top edge (0 = sharp)

# dovetail tabs (+X, +Y edges) and sockets (-X, -Y edges)
OFF = 29.0           # tab / socket centre distance from the plate corner
TAB_NECK = 9.2       # sharp-polygon width at the plate edge
TAB_TIP = 31.6       # sharp-polygon width at the tip
TAB_DEPTH = 12.0
NOTCH_OPEN = 11.8
NOTCH_BACK = 33.6
NOTCH_DEPTH = 12.0
R_TIP = 2.0          # rounding of the wide (outer) dovetail corners
R_BASE = 1.3         # rounding where the dovetail meets the plate edge

# spring clips (4 per side, centred) - compliant serpentine cut into the edge
CLIP_N = 4
CLIP_PITCH = 21.0
CLIP_W = 18.0        # slot width along the edge
CLIP_D = 13.8        # slot depth into the slab
BAR_OUT = 3.8        # clip bar protrudes this far beyond the slab edge
BAR_U0 = -8.6        # clip bar extent along the edge (local u)
BAR_U1 = 7.8
CLIP_S = 1.8         # spring strip width
V_MID = 3.5          # centre line of the middle stroke (from slab edge)
V_IN = 10.8          # centre line of the inner stroke
V_BAR = -0.9         # virtual centre line where the first bend enters the bar
CLIP_GAP = 0.5       # clearance between spring and slot wall
BAR_RV = 1.0         # rounding of the clip bar vertical edges
BAR_R = 0.4          # rounding of the clip bar top edges

# bosses and holes
BOSS_C_D = 18.0      # central pin
BOSS_H = 10.0
BOSS_S_D = 12.5      # two threaded standoffs
BOSS_S_HOLE = 6.0
BOSS_S_X = 18.0
BOSS_S_Y = -72.5
BOSS_S_FIL = 2.0      # radial width of the standoff flare
BOSS_S_FIL_H = 3.5    # height of the standoff flare
HOLE_D = 5.5
HOLE_R = 40.0

h = L / 2.0


# ---------------------------------------------------------------------------
# outline helpers
# ---------------------------------------------------------------------------
def outline_points():
    """Closed CCW polygon (x, y, corner radius)."""
    rt, rb = R_TIP, R_BASE
    pts = []
    # bottom edge (-Y): sockets
    pts.append((-h, -h, RC))
    for xc in (-h + OFF, h - OFF):
        pts += [(xc - NOTCH_OPEN / 2, -h, rb),
                (xc - NOTCH_BACK / 2, -h + NOTCH_DEPTH, rt),
                (xc + NOTCH_BACK / 2, -h + NOTCH_DEPTH, rt),
                (xc + NOTCH_OPEN / 2, -h, rb)]
    # right edge (+X): tabs
    pts.append((h, -h, RC))
    for yc in (-h + OFF, h - OFF):
        pts += [(h, yc - TAB_NECK / 2, rb),
                (h + TAB_DEPTH, yc - TAB_TIP / 2, rt),
                (h + TAB_DEPTH, yc + TAB_TIP / 2, rt),
                (h, yc + TAB_NECK / 2, rb)]
    # top edge (+Y): tabs
    pts.append((h, h, RC))
    for xc in (h - OFF, -h + OFF):
        pts += [(xc + TAB_NECK / 2, h, rb),
                (xc + TAB_TIP / 2, h + TAB_DEPTH, rt),
                (xc - TAB_TIP / 2, h + TAB_DEPTH, rt),
                (xc - TAB_NECK / 2, h, rb)]
    # left edge (-X): sockets
    pts.append((-h, h, RC))
    for yc in (h - OFF, -h + OFF):
        pts += [(-h, yc + NOTCH_OPEN / 2, rb),
                (-h + NOTCH_DEPTH, yc + NOTCH_BACK / 2, rt),
                (-h + NOTCH_DEPTH, yc - NOTCH_BACK / 2, rt),
                (-h, yc - NOTCH_OPEN / 2, rb)]
    return pts


def rounded_polygon_wire(pts):
    """Build a closed wire of lines and tangent arcs from (x, y, r) vertices."""
    n = len(pts)
    segs = []
    for i in range(n):
        px, py, r = pts[i]
        ax, ay, _ = pts[i - 1]
        bx, by, _ = pts[(i + 1) % n]
        d1 = (ax - px, ay - py)
        d2 = (bx - px, by - py)
        l1 = math.hypot(*d1)
        l2 = math.hypot(*d2)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        half = math.acos(cosang) / 2.0
        dist = r / math.tan(half)
        t1 = (px + d1[0] * dist, py + d1[1] * dist)
        t2 = (px + d2[0] * dist, py + d2[1] * dist)
        ux, uy = d1[0] + d2[0], d1[1] + d2[1]
        ul = math.hypot(ux, uy)
        ux, uy = ux / ul, uy / ul
        cdist = r / math.sin(half)
        cx, cy = px + ux * cdist, py + uy * cdist
        mid = (cx - ux * r, cy - uy * r)
        segs.append((t1, mid, t2))
    V = lambda p: cq.Vector(p[0], p[1], 0)
    edges = []
    for i in range(n):
        t1, mid, t2 = segs[i]
        edges.append(cq.Edge.makeThreePointArc(V(t1), V(mid), V(t2)))
        nt1 = segs[(i + 1) % n][0]
        edges.append(cq.Edge.makeLine(V(t2), V(nt1)))
    return cq.Wire.assembleEdges(edges)


def prism(wire, z0, z1):
    face = cq.Face.makeFromWires(wire)
    face = face.translate(cq.Vector(0, 0, z0))
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0)))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------------------------------------------------------------------
# slab with dovetail outline
# ---------------------------------------------------------------------------
outer_wire = rounded_polygon_wire(outline_points())
body = prism(outer_wire, 0.0, H)
if TOP_R > 0:
    body = body.faces(">Z").edges().fillet(TOP_R)


# ---------------------------------------------------------------------------
# spring clips: built for the -Y edge in local (u along edge, v inward)
# ---------------------------------------------------------------------------
S = CLIP_S
RL = (V_MID - V_BAR) / 2             # bend radii (centre line)
RR = (V_IN - V_MID) / 2
VL = (V_MID + V_BAR) / 2             # bend centres (v)
VR = (V_IN + V_MID) / 2
UL = -CLIP_W / 2 + CLIP_GAP + RL + S / 2
UR = CLIP_W / 2 - CLIP_GAP - RR - S / 2


def half_ring(uc, vc, r_mid, side):
    """Half annulus (strip width S), full slab height, bulging toward side."""
    ro, ri = r_mid + S / 2, r_mid - S / 2
    ring = (cq.Workplane("XY").center(uc, vc)
            .circle(ro).circle(ri).extrude(H))
    if side < 0:
        keep = box(uc - ro - 1, uc, vc - ro - 1, vc + ro + 1, -1, H + 1)
    else:
        keep = box(uc, uc + ro + 1, vc - ro - 1, vc + ro + 1, -1, H + 1)
    return ring.intersect(keep)


def clip_local():
    bar = box(BAR_U0, BAR_U1, -BAR_OUT, 0.0, 0.0, H)
    bar = bar.edges("|Z").fillet(BAR_RV).faces(">Z").edges().fillet(BAR_R)
    spring = (bar
              .union(half_ring(UL, VL, RL, -1))
              .union(box(UL, UR, V_MID - S / 2, V_MID + S / 2, 0, H))
              .union(half_ring(UR, VR, RR, +1))
              .union(box(-CLIP_W / 2 - 1.0, UR, V_IN - S / 2, V_IN + S / 2, 0, H)))
    cutter = box(-CLIP_W / 2, CLIP_W / 2, -5, CLIP_D, -1, H + 1)
    return spring, cutter


clip_solid, clip_cut = clip_local()
adds = []
cuts = []
for side in range(4):
    ang = 90.0 * side
    for i in range(CLIP_N):
        uc = (i - (CLIP_N - 1) / 2.0) * CLIP_PITCH
        cuts.append(clip_cut.translate((uc, -h, 0)).rotate((0, 0, 0), (0, 0, 1), ang))
        adds.append(clip_solid.translate((uc, -h, 0)).rotate((0, 0, 0), (0, 0, 1), ang))

for c in cuts:
    body = body.cut(c)
for a_ in adds:
    body = body.union(a_)


# ---------------------------------------------------------------------------
# bosses and holes
# ---------------------------------------------------------------------------
SEAM_BACK = 135.0    # put cylinder seams on the far side of the default view
SEAM_FRONT = -45.0   # hole seams on the near side (hidden by the rim)


def revolved_boss(r_out, height, fil_r=0.0, fil_h=0.0):
    """Solid boss; with fil_r > 0 the flank is one smooth revolved spline:
    an elliptical flare (fil_r wide, fil_h tall) running into the cylinder."""
    z0 = H - 1.0
    wp = cq.Workplane("XZ").moveTo(0.0, z0)
    if fil_r > 0:
        t = math.radians(45.0)
        pm = (r_out + fil_r * (1 - math.sin(t)), H + fil_h * (1 - math.cos(t)))
        tm = (-fil_r * math.cos(t), fil_h * math.sin(t))
        tl = math.hypot(*tm)
        tm = (tm[0] / tl, tm[1] / tl)
        wp = (wp.lineTo(r_out + fil_r, z0).lineTo(r_out + fil_r, H)
              .spline([pm, (r_out, H + fil_h), (r_out, H + height)],
                      tangents=[(-1.0, 0.0), tm, (0.0, 1.0), (0.0, 1.0)],
                      includeCurrent=True))
    else:
        wp = wp.lineTo(r_out, z0).lineTo(r_out, H + height)
    wp = wp.lineTo(0.0, H + height).close()
    return wp.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_BACK)


def hole_tool(d, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).circle(d / 2).extrude(z1 - z0)
            .rotate((0, 0, 0), (0, 0, 1), SEAM_FRONT))


body = body.union(revolved_boss(BOSS_C_D / 2, BOSS_H))
for sx in (-1, 1):
    p = (sx * BOSS_S_X, BOSS_S_Y, 0)
    body = body.union(revolved_boss(BOSS_S_D / 2, BOSS_H, BOSS_S_FIL, BOSS_S_FIL_H).translate(p))
    body = body.cut(hole_tool(BOSS_S_HOLE, H + 0.5, H + BOSS_H + 1).translate(p))

for (hx, hy) in ((HOLE_R, 0), (-HOLE_R, 0), (0, HOLE_R), (0, -HOLE_R)):
    body = body.cut(hole_tool(HOLE_D, -1, H + 1).translate((hx, hy, 0)))

result = body
